import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
ARM_LEN = 35.3        # straight arm length: -X end of part to centre of U bend
W_ARM = 5.0           # width of the bar (Y) on each arm
R_OUT = 14.6          # outer radius of the U bend
R_IN = R_OUT - W_ARM  # inner radius of the U bend
H_BAR = 6.0           # bar thickness (Z)
LEG_LEN = 16.0        # leg length below the bar
Z_TOP = LEG_LEN + H_BAR
PRONG = 5.0           # width (X) of each prong of the forked leg
SLOT = 5.0            # width (X) of the slot between the prongs
BEND_R = 4.6          # outer radius of the bar -> leg bend
R_OUTER_TOP = 2.5     # round on the outer top edge of the bar / outer leg edge
R_INNER_TOP = 0.9     # round on the inner top edge
R_BOTTOM = 1.0        # round on the outside underside edge of the bar
R_TIP = 0.9           # round on the tip of the outer prongs
NOTCH_X = 24.5        # notch centre measured from the -X end
NOTCH_W = 2.5
NOTCH_D = 2.5

EPS = 1e-3
OVERLAP = R_BOTTOM + 0.5   # how far the prong blocks reach up into the bar


def sel(pred):
    """Selector built from a predicate on an object's bounding box."""
    class _S(cq.Selector):
        def filter(self, objs):
            return [o for o in objs if pred(o.BoundingBox())]
    return _S()


def on_plane_y(b, y):
    return abs(b.ymin - y) < EPS and abs(b.ymax - y) < EPS


# ---------------- U shaped bar ----------------
bar = (
    cq.Workplane("XY", origin=(0, 0, LEG_LEN))
    .moveTo(0, -R_OUT)
    .lineTo(ARM_LEN, -R_OUT)
    .threePointArc((ARM_LEN + R_OUT, 0), (ARM_LEN, R_OUT))
    .lineTo(0, R_OUT)
    .lineTo(0, R_IN)
    .lineTo(ARM_LEN, R_IN)
    .threePointArc((ARM_LEN + R_IN, 0), (ARM_LEN, -R_IN))
    .lineTo(0, -R_IN)
    .close()
    .extrude(H_BAR)
)

# round on the outside underside edge of the bar (the inside underside edge stays sharp)


def outer_bottom_edge(b):
    if b.zmax > LEG_LEN + EPS or b.xmax < 1.0:
        return False
    side = on_plane_y(b, R_OUT) or on_plane_y(b, -R_OUT)
    u_arc = b.xmax > ARM_LEN + R_OUT - EPS
    return side or u_arc


bar = bar.edges(sel(outer_bottom_edge)).fillet(R_BOTTOM)

# ---------------- outer prongs (the bar turned down) ----------------
body = bar
for s in (-1, 1):
    y0, y1 = sorted((s * R_IN, s * R_OUT))
    leg = (
        cq.Workplane("XY")
        .box(PRONG, y1 - y0, LEG_LEN + OVERLAP, centered=False)
        .translate((0, y0, 0))
    )
    body = body.union(leg)
body = body.clean()

# bend between bar top and the -X end face
body = body.edges(sel(lambda b: b.xmax < EPS and b.zmin > Z_TOP - EPS)).fillet(BEND_R)


# large round on the outside top edge, running round the bends and down the legs
def outer_edge(b):
    side = on_plane_y(b, R_OUT) or on_plane_y(b, -R_OUT)
    along = side and (b.zmax > Z_TOP - EPS or b.xmax < BEND_R + EPS)
    u_arc = b.xmax > ARM_LEN + R_OUT - EPS and b.zmin > Z_TOP - EPS
    return along or u_arc


body = body.edges(sel(outer_edge)).fillet(R_OUTER_TOP)


# small round on the inside top edge
def inner_edge(b):
    side = on_plane_y(b, R_IN) or on_plane_y(b, -R_IN)
    along = side and (b.zmax > Z_TOP - EPS or b.xmax < BEND_R + EPS) and b.xmin < ARM_LEN - 1
    u_arc = abs(b.xmax - (ARM_LEN + R_IN)) < EPS and b.zmin > Z_TOP - EPS
    return along or u_arc


body = body.edges(sel(inner_edge)).fillet(R_INNER_TOP)

# rounded tip of the outer prongs (the slot-facing edge stays sharp)
body = body.edges(sel(lambda b: b.zmax < EPS and not b.xmin > PRONG - EPS)).fillet(R_TIP)

# ---------------- inner prongs (sharp blocks) ----------------
x_inner = PRONG + SLOT
for s in (-1, 1):
    y0, y1 = sorted((s * R_IN, s * R_OUT))
    blk = (
        cq.Workplane("XY")
        .box(PRONG, y1 - y0, LEG_LEN + OVERLAP, centered=False)
        .translate((x_inner, y0, 0))
    )
    # square off the bar underside above the slot (slot roof has sharp edges)
    roof = (
        cq.Workplane("XY")
        .box(SLOT + PRONG, y1 - y0, OVERLAP, centered=False)
        .translate((PRONG, y0, LEG_LEN))
    )
    body = body.union(blk).union(roof)

# ---------------- square notches across the top of both arms ----------------
notch = (
    cq.Workplane("XY")
    .box(NOTCH_W, 2 * R_OUT + 4, NOTCH_D + 1.0, centered=(True, True, False))
    .translate((NOTCH_X, 0, Z_TOP - NOTCH_D))
)
body = body.cut(notch).clean()

result = body
